"""Cast corner block: a rounded 46 x 50 x 46 block with three crossing (non-intersecting)
through holes, the (-X,+Y,-Z) corner cut away by three tapered chamfers plus a truncation
face (which carries a blind hole), and a 45 deg pocket sunk into the +X/+Z edge at the back."""
import cadquery as cq
from cadquery.occ_impl.geom import Matrix
from OCP.BRepFilletAPI import BRepFilletAPI_MakeFillet
from OCP.TopTools import TopTools_IndexedDataMapOfShapeListOfShape
from OCP.TopExp import TopExp
from OCP.TopAbs import TopAbs_EDGE, TopAbs_FACE
from OCP.TopoDS import TopoDS

# ---------------- driving dimensions (mm) ----------------
LX, LY, LZ = 46.0, 50.0, 46.0
R_EDGE = 5.0          # general edge rounding
R_CH = 7.0            # rounding between a tapered chamfer and a block face
R_CH_T = 5.0          # rounding between a tapered chamfer and the truncation face
R_T = 7.0             # rounding between the truncation face and a block face
HOLE_D = 9.5          # the three fixing holes
HOLE_RIM = 0.7        # rounding of the hole rims

# hole positions
ZH = (13.0, -4.5)     # vertical hole (x, y)
XH = (-15.2, 13.1)    # hole along X (y, z)
YH = (2.0, -13.6)     # hole along Y (x, z)

# tapered chamfers on the three edges meeting at the (-X,+Y,-Z) corner
V_LEG_TOP = 22.5      # vertical edge (-X,+Y): leg at the top face
V_TAPER = 0.68        #   leg lost per mm going down
W_LEG_FRONT = 15.0    # edge (-X,-Z): leg at the front face
W_TAPER = 0.80        #   leg lost per mm going back
U_LEG_RIGHT = 20.7    # edge (+Y,-Z): leg at the right face
U_TAPER = 0.50        #   leg lost per mm going left
T_D = 27.0            # corner truncation plane  -x + y - z = T_D (origin at centre)

# blind hole entering from the truncation face (parallel to Y)
BH_D = 8.5
BH_XZ = (-4.1, -4.8)
BH_DEPTH = 10.0

# notch (45 deg elliptic bore into the +X/+Z edge near the back)
NOTCH_A = 4.75        # semi-axis along the edge (Y)
NOTCH_B = 5.75        # semi-axis across the edge
NOTCH_C = 5.0         # depth of the rounded end
NOTCH_Y = 17.2
NOTCH_DEPTH = 11.0    # from the sharp edge line to the start of the rounded end

hx, hy, hz = LX / 2, LY / 2, LZ / 2


def halfspace_cut(solid, point, normal, size=400.0):
    """remove everything on the +normal side of the plane through point"""
    n = cq.Vector(*normal).normalized()
    ref = cq.Vector(1, 0, 0) if abs(n.x) < 0.9 else cq.Vector(0, 1, 0)
    xd = ref.cross(n).normalized()
    pl = cq.Plane(origin=cq.Vector(*point), xDir=xd, normal=n)
    blk = cq.Workplane(pl).rect(size, size).extrude(size)
    return solid.cut(blk)


body = cq.Workplane("XY").box(LX, LY, LZ)

# V: (x+hx) + (hy-y) >= V_LEG_TOP - V_TAPER*(hz - z)
body = halfspace_cut(body, (-hx + V_LEG_TOP, hy, hz), (-1, 1, V_TAPER))
# W: (x+hx) + (z+hz) >= W_LEG_FRONT - W_TAPER*(y + hy)
body = halfspace_cut(body, (-hx + W_LEG_FRONT, -hy, -hz), (-1, -W_TAPER, -1))
# U: (hy-y) + (z+hz) >= U_LEG_RIGHT - U_TAPER*(hx - x)
body = halfspace_cut(body, (hx, hy - U_LEG_RIGHT, -hz), (U_TAPER, 1, -1))
# T: corner truncation
body = halfspace_cut(body, (0, T_D, 0), (-1, 1, -1))

# rounding, all edges in one blend with a radius chosen by the pair of faces they join:
#   tapered chamfer / block face -> R_CH, chamfer / truncation -> R_CH_T,
#   truncation / block face -> R_T, block / block -> R_EDGE
cut_normals = {"V": cq.Vector(-1, 1, V_TAPER).normalized(),
               "W": cq.Vector(-1, -W_TAPER, -1).normalized(),
               "U": cq.Vector(U_TAPER, 1, -1).normalized(),
               "T": cq.Vector(-1, 1, -1).normalized()}


def face_kind(face):
    n = face.normalAt()
    for k, c in cut_normals.items():
        if (n - c).Length < 1e-3:
            return k
    return "B"


def edge_radius(kinds):
    if "T" in kinds:
        return R_T if kinds.count("B") == 1 else R_CH_T
    if kinds.count("B") == 1:
        return R_CH
    return R_EDGE


solid = body.val()
emap = TopTools_IndexedDataMapOfShapeListOfShape()
TopExp.MapShapesAndAncestors_s(solid.wrapped, TopAbs_EDGE, TopAbs_FACE, emap)
blend = BRepFilletAPI_MakeFillet(solid.wrapped)
for i in range(1, emap.Extent() + 1):
    kinds = [face_kind(cq.Face(TopoDS.Face_s(f))) for f in emap.FindFromIndex(i)]
    blend.Add(edge_radius(kinds), TopoDS.Edge_s(emap.FindKey(i)))
blend.Build()
if blend.IsDone():
    body = cq.Workplane("XY").add(cq.Shape.cast(blend.Shape()))
else:  # fall back to a single radius if the kernel refuses the mixed blend
    body = body.edges().fillet(R_EDGE)

# notch : 45 deg elliptic bore into the +X/+Z edge with a rounded (half-ellipsoid) end
ax = cq.Vector(1, 0, 1).normalized()
npl = cq.Plane(origin=cq.Vector(hx, NOTCH_Y, hz), xDir=cq.Vector(0, 1, 0), normal=ax)
notch = (cq.Workplane(npl).workplane(offset=-NOTCH_DEPTH)
         .ellipse(NOTCH_A, NOTCH_B).extrude(NOTCH_DEPTH + 30))
cap = (cq.Solid.makeSphere(1.0, angleDegrees1=-90, angleDegrees2=90)
       .transformGeometry(Matrix([[NOTCH_A, 0, 0, 0], [0, NOTCH_B, 0, 0], [0, 0, NOTCH_C, 0]]))
       .moved(cq.Location(cq.Vector(0, 0, -NOTCH_DEPTH)))
       .moved(cq.Location(npl)))
notch = notch.union(cq.Workplane("XY").add(cap))
body = body.cut(notch)

# through holes
L = 200
hzc = cq.Workplane("XY").circle(HOLE_D / 2).extrude(L).translate((ZH[0], ZH[1], -L / 2))
hxc = cq.Workplane("YZ").circle(HOLE_D / 2).extrude(L).translate((-L / 2, XH[0], XH[1]))
hyc = cq.Workplane("XZ").circle(HOLE_D / 2).extrude(L).translate((YH[0], L / 2, YH[1]))
body = body.cut(hzc).cut(hxc).cut(hyc)

# soften the hole rims (one closed rim edge per opening)
def rim_edges(shape):
    sel = []
    for f in shape.faces().vals():
        if f.geomType() == "CYLINDER":
            r = f._geomAdaptor().Cylinder().Radius()
            if abs(r - HOLE_D / 2) < 0.05:
                sel.extend(e for e in f.Edges() if e.geomType() != "LINE")
    return sel


try:
    body = body.newObject(rim_edges(body)).fillet(HOLE_RIM)
except Exception as exc:  # keep the sharp rims if the kernel refuses
    print("rim fillet skipped:", exc)

# blind hole from the truncation face
y_t = T_D + BH_XZ[0] + BH_XZ[1]          # where its axis meets the T plane
bh = (cq.Workplane("XZ", origin=(BH_XZ[0], y_t + 20, BH_XZ[1]))
      .circle(BH_D / 2).extrude(20 + BH_DEPTH))   # XZ normal is -Y: runs from y_t+20 down to y_t-depth
body = body.cut(bh)

result = body
